import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 179.0          # overall width  (X)
D = 117.0          # overall depth  (Y)
H = 200.0          # overall height (Z)
T = 4.5            # wall thickness
TF = 3.0           # floor thickness
R_OUT = 7.0        # vertical edge radius

Y_PAN = 51.8       # front face of the inner (motherboard) tray
T_PAN = 5.0        # tray thickness
X_COL = 129.4      # -X face of the right-back column wall (P1)
T_COL = 4.5
Z_COL = 23.3       # bottom of the right column wall
X_LCOL = 13.7      # +X face of the left-back column wall (P2)
Z_LCOL = 33.4      # bottom of the left column wall

BOSS_D = 19.0      # boss on the top plate
BOSS_ID = 16.0
BOSS_H = 1.6
BOSS_X, BOSS_Y = 154.0, 96.5

FAN_Y = 84.5
FAN_X = (51.6, 119.4)

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- helpers ----------------
def hex_profile(u0, u1, zb, zs, zt, flat):
    """outline (u,z): vertical sides, chamfered top rising to a centred flat top"""
    uc = 0.5 * (u0 + u1)
    return [(u0, zb), (u1, zb), (u1, zs), (uc + flat / 2, zt), (uc - flat / 2, zt), (u0, zs)]


def rounded_outline(wp, pts, radii):
    """closed outline through pts with a fillet of radius radii[i] at vertex i"""
    n = len(pts)
    segs = []
    for i in range(n):
        p = pts[i]
        r = radii[i]
        if r <= 0:
            segs.append((p, None, None))
            continue
        a, b = pts[i - 1], pts[(i + 1) % n]
        d1 = (p[0] - a[0], p[1] - a[1])
        l1 = math.hypot(*d1)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (b[0] - p[0], b[1] - p[1])
        l2 = math.hypot(*d2)
        d2 = (d2[0] / l2, d2[1] / l2)
        cosang = max(-1.0, min(1.0, -(d1[0] * d2[0] + d1[1] * d2[1])))
        th = math.acos(cosang)
        t = r / math.tan(th / 2)
        A = (p[0] - d1[0] * t, p[1] - d1[1] * t)
        B = (p[0] + d2[0] * t, p[1] + d2[1] * t)
        bis = (-d1[0] + d2[0], -d1[1] + d2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        k = r / math.sin(th / 2) - r
        M = (p[0] + bis[0] * k, p[1] + bis[1] * k)
        segs.append((A, M, B))
    start = segs[0][0]
    wp = wp.moveTo(*start)
    if segs[0][1] is not None:
        wp = wp.threePointArc(segs[0][1], segs[0][2])
    for A, M, B in segs[1:]:
        wp = wp.lineTo(*A)
        if M is not None:
            wp = wp.threePointArc(M, B)
    return wp.close()


def prism(plane, pts, depth, origin, rb=0.0, radii=None):
    if radii is None:
        radii = [rb, rb] + [0.0] * (len(pts) - 2)
    wp = cq.Workplane(plane, origin=origin)
    return rounded_outline(wp, pts, radii).extrude(depth)


def cut_x_wall(body, pts, x0, depth, rb=0.0, radii=None):
    # YZ plane: local x = Y, local y = Z, extrudes towards +X
    return body.cut(prism("YZ", pts, depth, (x0, 0, 0), rb, radii))


def cut_y_wall(body, pts, y0, depth, rb=0.0, radii=None):
    # XZ plane: local x = X, local y = Z, extrudes towards -Y
    return body.cut(prism("XZ", pts, depth, (0, y0, 0), rb, radii))


def block(x0, y0, z0, dx, dy, dz):
    return cq.Workplane("XY").box(dx, dy, dz, centered=False).translate((x0, y0, z0))


# ---------------- outer shell (open top) ----------------
outer = cq.Workplane("XY").box(W, D, H, centered=False).edges("|Z").fillet(R_OUT)
inner = block(T, T, TF, W - 2 * T, D - 2 * T, H).edges("|Z").fillet(R_OUT - T)
body = outer.cut(inner)

# ---------------- inner tray wall, full width ----------------
body = body.union(block(T, Y_PAN, TF, W - 2 * T, T_PAN, H - TF))

# right-back column: hanging wall P1 + top plate
y_c0 = Y_PAN + T_PAN
p1 = block(X_COL, y_c0, Z_COL, T_COL, D - T - y_c0, H - Z_COL)
p1 = p1.edges("|X").edges("<Z").edges(">Y").fillet(16.0)
p1 = p1.edges("|X").edges("<Z").edges("<Y").fillet(6.0)
# pentagon window in P1
p1 = p1.cut(prism("YZ", hex_profile(63.6, 104.3, 28.5, 40.3, 49.5, 7.2), T_COL + 2, (X_COL - 1, 0, 0)))
body = body.union(p1)
body = body.union(block(X_COL, Y_PAN, H - T, W - T - X_COL, D - T - Y_PAN, T))

# left-back column: wall P2 + top strip
body = body.union(block(X_LCOL - T, y_c0, Z_LCOL, T, D - T - y_c0, H - Z_LCOL))
# concave fillet where P2 meets the back wall
R_IN = 3.0
fil = block(X_LCOL, D - T - R_IN, Z_LCOL, R_IN, R_IN, H - Z_LCOL).cut(
    cq.Workplane("XY", origin=(0, 0, Z_LCOL - 1)).center(X_LCOL + R_IN, D - T - R_IN).circle(R_IN).extrude(H)
)
body = body.union(fil)
body = body.union(block(T, Y_PAN, H - T, X_LCOL - T, D - T - Y_PAN, T))

# ---------------- front opening (gable top) ----------------
FO_X = 6.5         # front opening side inset
body = cut_y_wall(body, hex_profile(FO_X, W - FO_X, 7.0, 164.0, 187.0, 11.6), T + 0.5, T + 1.5)

# ---------------- back wall openings ----------------
body = cut_y_wall(body, hex_profile(13.4, 130.7, 67.0, 151.0, 187.0, 10.0), D + 1.0, T + 2.0, rb=10.0)
body = cut_y_wall(body, hex_profile(X_COL + T_COL, W - T, 66.0, 167.0, 186.0, 4.0), D + 1.0, T + 2.0, rb=8.0)
body = cut_y_wall(body, [(11.0, TF), (W - T, TF), (W - T, 37.0), (11.0, 37.0)], D + 1.0, T + 2.0)

# ---------------- side wall openings ----------------
UF = hex_profile(13.4, 41.0, 115.8, 175.5, 189.2, 7.0)       # upper front
LF = hex_profile(R_OUT, Y_PAN, 13.4, 88.1, 101.9, 7.7)       # lower front
for x0 in (W - T - 1.0, -1.0):
    body = cut_x_wall(body, UF, x0, T + 2, rb=7.0)
    body = cut_x_wall(body, LF, x0, T + 2, rb=13.0)
# +X side: back openings
YB0 = Y_PAN + T_PAN   # back openings start flush with the back of the tray
body = cut_x_wall(body, hex_profile(YB0, 111.0, 125.3, 179.3, 193.4, 6.1), W - T - 1.0, T + 2,
                  radii=[14.0, 12.0, 0, 0, 0, 0])
body = cut_x_wall(body, hex_profile(YB0, 111.4, 12.8, 90.9, 111.1, 6.5), W - T - 1.0, T + 2, rb=11.0)
# -X side: back openings (lower than on +X)
body = cut_x_wall(body, hex_profile(YB0, 109.8, 90.0, 139.0, 153.0, 3.0), -1.0, T + 2,
                  radii=[17.0, 7.0, 0, 0, 0, 0])
body = cut_x_wall(body, hex_profile(YB0, 111.4, 12.8, 57.0, 71.4, 3.0), -1.0, T + 2, rb=11.0)

# through holes along X at the back columns
for z in (159.5, 78.5):
    body = body.cut(cq.Workplane("YZ", origin=(-1, 0, 0)).center(86.0, z).circle(2.0).extrude(W + 2))
# holes in the back wall, in line with the tray holes
for z in (161.3, 59.7):
    body = body.cut(cq.Workplane("XZ", origin=(0, D + 1, 0)).center(14.0, z).circle(2.0).extrude(T + 2))
# small holes low in the side walls
body = body.cut(cq.Workplane("YZ", origin=(-1, 0, 0)).center(62.8, 7.8).circle(1.5).extrude(W + 2))


# ---------------- tray slots ----------------
def bullet(xc, w=11.4, zb=13.8, zs=28.2, zt=34.4):
    return [(xc - w / 2, zb), (xc + w / 2, zb), (xc + w / 2, zs), (xc + 0.8, zt), (xc - 0.8, zt), (xc - w / 2, zs)]


pitch = 17.6
for i in range(8):
    xc = 25.9 + pitch * i
    if i == 6:
        pts = [(xc - 5.7, 13.8), (xc + 5.7, 13.8), (xc + 5.7, 24.3), (xc - 5.7, 24.3)]
    else:
        pts = bullet(xc)
    body = cut_y_wall(body, pts, Y_PAN + T_PAN + 1.0, T_PAN + 2.0, rb=1.0)

# window in the tray top right, into the column
body = cut_y_wall(body, [(X_COL + T_COL, 166.0), (W - T, 166.0), (W - T, H - T), (X_COL + T_COL, H - T)],
                  Y_PAN + T_PAN + 1.0, T_PAN + 2.0)

# tray mounting holes
for (hx, hz) in ((14.0, 161.3), (165.0, 161.0), (14.0, 59.7), (165.0, 10.3)):
    body = body.cut(cq.Workplane("XZ", origin=(0, Y_PAN + T_PAN + 1, 0)).center(hx, hz).circle(2.0).extrude(T_PAN + 2))

# ---------------- top boss (thin tube) ----------------
boss = cq.Workplane("XY", origin=(0, 0, H)).center(BOSS_X, BOSS_Y).circle(BOSS_D / 2).circle(BOSS_ID / 2).extrude(BOSS_H)
body = body.union(boss)
body = body.cut(cq.Workplane("XY", origin=(0, 0, H - T - 1)).center(BOSS_X, BOSS_Y).circle(BOSS_ID / 2).extrude(T + 2))


# ---------------- floor cut-outs ----------------
def floor_rect(x0, x1, y0, y1):
    return cq.Workplane("XY", origin=(0, 0, -1)).center((x0 + x1) / 2, (y0 + y1) / 2).rect(x1 - x0, y1 - y0).extrude(TF + 2)


for (x0, x1, y0, y1) in ((11.0, 24.8, 14.3, 32.6), (28.8, 50.7, 23.5, 32.9), (53.3, 75.5, 9.8, 32.9),
                         (79.5, 100.4, 22.3, 34.0), (104.3, 127.5, 13.1, 32.9)):
    body = body.cut(floor_rect(x0, x1, y0, y1))

# jack pocket with two holes
body = body.cut(cq.Workplane("XY", origin=(0, 0, TF - 1.5)).center(145.5, 30.0).rect(32.6, 13.1).extrude(3))
for hx in (137.0, 152.0):
    body = body.cut(cq.Workplane("XY", origin=(0, 0, -1)).center(hx, 30.1).circle(5.2).extrude(TF + 2))


# fan grilles
def fan_cut(cx, cy, r_hub=10.0, r_in=13.4, r_out=24.4, spoke=2.4, pitch_h=43.4, hole_d=4.4):
    ring = cq.Workplane("XY", origin=(0, 0, -1)).center(cx, cy).circle(r_out).circle(r_in).extrude(TF + 2)
    for k in range(4):
        bar = (
            cq.Workplane("XY", origin=(0, 0, -2)).center(cx, cy).rect(2 * r_out + 4, spoke).extrude(TF + 4)
            .rotate((cx, cy, 0), (cx, cy, 1), k * 45.0)
        )
        ring = ring.cut(bar)
    cutter = ring.union(cq.Workplane("XY", origin=(0, 0, -1)).center(cx, cy).circle(r_hub).extrude(TF + 2))
    for sx in (-1, 1):
        for sy in (-1, 1):
            cutter = cutter.union(
                cq.Workplane("XY", origin=(0, 0, -1)).center(cx + sx * pitch_h / 2, cy + sy * pitch_h / 2)
                .circle(hole_d / 2).extrude(TF + 2)
            )
    return cutter


for fx in FAN_X:
    body = body.cut(fan_cut(fx, FAN_Y))

result = body
